import cadquery as cq

# ------------------------------------------------------------------
# Solid ball (plain sphere) -- all six reference views show a
# featureless sphere with equal extents along X, Y and Z.
# ------------------------------------------------------------------

# Driving dimensions (mm)
DIAMETER = 50.0                 # ball diameter
RADIUS = DIAMETER / 2.0

# The B-rep sphere has one periodic seam meridian (at +X, running
# pole to pole along Z).  Orienting it is purely cosmetic (the
# geometry is rotation invariant): lay it horizontal (about X) and
# turn it to the back-left so it faces away from the default camera.
SEAM_LAY_DEG = 90.0             # rotation about X
SEAM_TURN_DEG = 135.0           # then rotation about Z

result = (
    cq.Workplane("XY")
    .sphere(RADIUS)
    .rotate((0, 0, 0), (1, 0, 0), SEAM_LAY_DEG)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_TURN_DEG)
)

VIEW = {"azimuth": 45, "elevation": 26}
